import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FL_R = 59.5          # flange outer radius
FL_T = 5.5           # flange thickness
EAR_DIST = 64.4      # bolt-ear centre distance from axis (on 45 deg diagonals)
EAR_R = 6.6          # ear lobe radius
EAR_HOLE_D = 5.9     # bolt hole diameter
EAR_BLEND_R = 5.0    # concave blend between ear and flange circle

CUP_DEPTH = 58.8     # from flange front face to back face of the cup
CUP_R = 50.0         # outer arc radius of the cup section (at flange front plane)
CUP_H = 42.5         # outer flat half-height of the cup section
CUP_BLEND = 5.0      # round on the creases between the flats and the conical sides
SIDE_DRAFT = 3.2     # draft of the conical (arc) sides of the cup (deg)
FLAT_DRAFT = 5.0     # draft of the flat top/bottom walls of the cup (deg)
BACK_FILLET = 11.0   # outer fillet around cup back face
ROOT_FILLET = 10.0   # fillet between flange and cup

IN_R = 40.5          # cavity arc radius (= flange opening)
IN_H = 32.0          # cavity flat half-height
IN_BLEND = 4.0       # blend between flat and arc of the cavity section
IN_DRAFT = 0.0       # draft of the cavity walls (deg)
BACK_WALL = 5.5      # thickness of the cup bottom
IN_FILLET = 10.0     # inner fillet at the cavity bottom

BH_X = 21.5          # back-wall hole pattern half spacing (x)
BH_Z = 16.0          # back-wall hole pattern half spacing (z)
BH_D = 5.5           # back-wall hole diameter

SLOT_W = 6.5         # split slot width (through top wall and back wall)
NOTCH_W = 11.0       # wider notch in the flange at the top
NOTCH_Z0 = 41.5      # notch taper lower end (height)
NOTCH_Z1 = 48.0      # notch taper upper end (height)

# Build coordinates: cup axis = +Z (becomes +Y), "up" = -Y (becomes +Z)


def clipped_circle(wp, r, h):
    """Circle of radius r cut by flats at +-h."""
    a = math.sqrt(r * r - h * h)
    return (wp.moveTo(-a, h).lineTo(a, h)
            .threePointArc((r, 0), (a, -h))
            .lineTo(-a, -h)
            .threePointArc((-r, 0), (-a, h))
            .close())


def drafted_pocket_body(R, h, depth, draft, crease_r, end_r, z0=0.0):
    """Clipped-circle section extruded along +Z with draft, flat/arc creases rounded,
    far end rounded."""
    wp = cq.Workplane("XY").workplane(offset=z0)
    solid = clipped_circle(wp, R, h).extrude(depth, taper=draft)
    solid = solid.edges("not(>Z or <Z)").fillet(crease_r)
    return solid.edges(">Z").fillet(end_r)


def flange_outline(wp):
    """Circle with four bolt ears on the diagonals, blended by concave arcs."""
    Rc = FL_R + EAR_BLEND_R
    cphi = (Rc ** 2 + EAR_DIST ** 2 - (EAR_R + EAR_BLEND_R) ** 2) / (2 * Rc * EAR_DIST)
    phi = math.acos(cphi)

    def pol(r, ang):
        return (r * math.cos(ang), r * math.sin(ang))

    ears = [math.radians(45 + 90 * k) for k in range(4)]
    pts = []
    for k, ea in enumerate(ears):
        E = pol(EAR_DIST, ea)
        for sgn in (-1, 1):
            ca = ea + sgn * phi
            C = pol(Rc, ca)
            P_big = pol(FL_R, ca)
            dx, dy = E[0] - C[0], E[1] - C[1]
            L = math.hypot(dx, dy)
            P_ear = (C[0] + EAR_BLEND_R * dx / L, C[1] + EAR_BLEND_R * dy / L)
            ux, uy = P_big[0] - C[0], P_big[1] - C[1]
            vx, vy = P_ear[0] - C[0], P_ear[1] - C[1]
            mx, my = ux + vx, uy + vy
            ml = math.hypot(mx, my)
            M = (C[0] + EAR_BLEND_R * mx / ml, C[1] + EAR_BLEND_R * my / ml)
            pts.append((P_big, M, P_ear, E))
    w = wp.moveTo(*pts[0][0])
    for k in range(4):
        Pb1, M1, Pe1, E = pts[2 * k]
        Pb2, M2, Pe2, _ = pts[2 * k + 1]
        ea = ears[k]
        w = w.threePointArc(M1, Pe1)
        w = w.threePointArc((E[0] + EAR_R * math.cos(ea), E[1] + EAR_R * math.sin(ea)), Pe2)
        w = w.threePointArc(M2, Pb2)
        a0 = ears[k] + phi
        a1 = ears[(k + 1) % 4] - phi
        if a1 < a0:
            a1 += 2 * math.pi
        w = w.threePointArc(pol(FL_R, 0.5 * (a0 + a1)), pts[(2 * k + 2) % 8][0])
    return w.close()


# ---- flange plate ----
flange = flange_outline(cq.Workplane("XY")).extrude(FL_T)

# ---- outer cup: revolved drafted cone (rounded bottom) intersected with a drafted slab ----
_R1 = CUP_R - CUP_DEPTH * math.tan(math.radians(SIDE_DRAFT))
_H1 = CUP_H - CUP_DEPTH * math.tan(math.radians(FLAT_DRAFT))
cone = (cq.Workplane("XZ")
        .polyline([(0, 0), (CUP_R, 0), (_R1, CUP_DEPTH), (0, CUP_DEPTH)]).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
cone = cone.faces(">Z").edges().fillet(BACK_FILLET)
slab = (cq.Workplane("YZ")
        .polyline([(-CUP_H, 0), (CUP_H, 0), (_H1, CUP_DEPTH), (-_H1, CUP_DEPTH)]).close()
        .extrude(FL_R + 5, both=True))
slab = slab.edges(">Z and |X").fillet(BACK_FILLET)
cup = cone.intersect(slab)


def _crease(e):
    c = e.Center()
    return 0.5 < c.z < CUP_DEPTH - 0.5 and abs(c.x) > 5 and abs(c.y) > 5


cup = cup.newObject([e for e in cup.edges().vals() if _crease(e)]).fillet(CUP_BLEND)

body = flange.union(cup)


# root fillet between flange back face and cup wall
def _root_edge(e):
    c = e.Center()
    return abs(c.z - FL_T) < 1e-3 and math.hypot(c.x, c.y) < FL_R - 5


root_edges = [e for e in body.edges().vals() if _root_edge(e)]
body = body.newObject(root_edges).fillet(ROOT_FILLET)

# ---- cavity ----
cav_depth = CUP_DEPTH - BACK_WALL
ext = 2.0
t = math.tan(math.radians(IN_DRAFT))
cavity = drafted_pocket_body(IN_R + ext * t, IN_H + ext * t, cav_depth + ext, IN_DRAFT,
                             IN_BLEND, IN_FILLET, z0=-ext)
body = body.cut(cavity)

# ---- ear bolt holes ----
ear_pts = [(EAR_DIST * math.cos(math.radians(45 + 90 * k)),
            EAR_DIST * math.sin(math.radians(45 + 90 * k))) for k in range(4)]
holes = (cq.Workplane("XY").workplane(offset=-1).pushPoints(ear_pts)
         .circle(EAR_HOLE_D / 2).extrude(FL_T + 2))
body = body.cut(holes)

# ---- back wall holes ----
bh_pts = [(sx * BH_X, sy * BH_Z) for sx in (-1, 1) for sy in (-1, 1)]
bholes = (cq.Workplane("XY").workplane(offset=cav_depth - 2).pushPoints(bh_pts)
          .circle(BH_D / 2).extrude(BACK_WALL + 6))
body = body.cut(bholes)

# ---- split slot (towards "up" = -Y in build coords) ----
top = FL_R + 10
slot = (cq.Workplane("XY").workplane(offset=-1)
        .moveTo(-SLOT_W / 2, 0).lineTo(-SLOT_W / 2, -top)
        .lineTo(SLOT_W / 2, -top).lineTo(SLOT_W / 2, 0)
        .threePointArc((0, SLOT_W / 2), (-SLOT_W / 2, 0)).close()
        .extrude(CUP_DEPTH + 2))
body = body.cut(slot)

# notch profile in final (x, z) coordinates: wide at the top, S-curve down to the slot width
_d = (NOTCH_W - SLOT_W) / 2.0
_L = NOTCH_Z1 - NOTCH_Z0
_th = 2.0 * math.atan2(_d, _L)
_r = (_L / 2.0) / math.sin(_th)


def _s_curve(side):
    """points (start, mid1, inflection, mid2, end) of the S-curve on one side (side=-1 left, +1 right)."""
    x0 = side * NOTCH_W / 2.0
    x1 = side * SLOT_W / 2.0
    c1x = x0 - side * _r
    c2x = x1 + side * _r
    m1 = (c1x + side * _r * math.cos(_th / 2), NOTCH_Z1 - _r * math.sin(_th / 2))
    pi = (c1x + side * _r * math.cos(_th), NOTCH_Z1 - _r * math.sin(_th))
    m2 = (c2x - side * _r * math.cos(_th / 2), NOTCH_Z0 + _r * math.sin(_th / 2))
    return (x0, NOTCH_Z1), m1, pi, m2, (x1, NOTCH_Z0)


def _b(p):  # final (x, z) -> build (x, -z)
    return (p[0], -p[1])


Ls, Lm1, Li, Lm2, Le = _s_curve(-1)
Rs, Rm1, Ri, Rm2, Re = _s_curve(1)
notch = (cq.Workplane("XY").workplane(offset=-1)
         .moveTo(*_b((-NOTCH_W / 2, top)))
         .lineTo(*_b(Ls))
         .threePointArc(_b(Lm1), _b(Li))
         .threePointArc(_b(Lm2), _b(Le))
         .lineTo(*_b(Re))
         .threePointArc(_b(Rm2), _b(Ri))
         .threePointArc(_b(Rm1), _b(Rs))
         .lineTo(*_b((NOTCH_W / 2, top)))
         .close()
         .extrude(CUP_DEPTH + 2))
body = body.cut(notch)

# rotate: build +Z (cup axis) -> +Y, build -Y ("up") -> +Z
result = body.rotate((0, 0, 0), (1, 0, 0), -90)

VIEW = {"azimuth": 45, "elevation": 26}
